import math
import cadquery as cq
from OCP.BRepOffsetAPI import BRepOffsetAPI_ThruSections
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeVertex
from OCP.gp import gp_Pnt
from OCP.Approx import Approx_ParametrizationType

# ---------------------------------------------------------------
# Organic "saddle cup" (tooth-crown like): a blunt, heart-shaped solid
# whose horizontal sections are stretched along the front-right /
# back-left diagonal, with a dished basin cut into its top that leaves
# a tall cusp at the front-left and a lower cusp at the back-right.
# Millimetres, Z up, bottom tip near Z = 0.
# ---------------------------------------------------------------

N_PTS = 16             # points per section spline
SEAM_ANGLE = 100.0     # polar angle where every section spline starts

# blunt bottom tip of the body
TIP = (-6.6, -6.9, -0.7)

# Body sections: (z, centre_x, centre_y, radii every 45 deg from +X, CCW)
BODY_SECTIONS = [
    (1.0, -5.55, -6.41, [4.20, 3.89, 5.58, 7.14, 7.37, 7.13, 6.52, 5.23]),
    (3.2, -5.79, -4.89, [6.09, 5.38, 7.55, 9.90, 9.18, 8.34, 8.63, 8.27]),
    (7.0, -6.25, -2.74, [9.34, 7.65, 10.30, 14.57, 10.90, 10.04, 10.54, 15.27]),
    (13.0, -6.74, -1.76, [13.47, 10.22, 14.94, 18.84, 14.46, 12.59, 14.74, 22.22]),
    (19.0, -6.02, -1.51, [17.09, 14.27, 19.06, 20.68, 17.33, 14.88, 17.79, 25.69]),
    (24.3, -4.90, 0.01, [22.12, 19.52, 23.40, 22.67, 19.78, 17.01, 20.25, 27.36]),
    (30.0, -3.41, 0.04, [25.13, 22.52, 25.00, 24.47, 21.49, 18.88, 21.12, 29.72]),
    (37.5, -1.72, 0.01, [26.10, 25.53, 25.68, 26.40, 22.95, 20.77, 23.40, 27.74]),
]

# Upper body (crown) outline: centre and radii every 22.5 deg, used for
# the straight-walled top part at the listed heights.
CROWN_CENTER = (-0.02, 0.22)
CROWN_RADII = [26.75, 27.02, 26.98, 24.87, 24.58, 25.34, 27.97, 27.58,
               25.03, 21.80, 21.34, 22.66, 23.86, 26.19, 28.40, 28.44]
CROWN_Z = [46.0, 55.0, 64.0]

# Basin cut: local frame (u along the low-rim axis, v across it, +v
# toward the back-right cusp).  Each station: (u, [(v, z), ...])
BASIN_ANGLE = -32.0            # direction of the basin axis (deg from +X)
BASIN_ORIGIN = (2.2, 2.5)      # a point on the basin axis (XY)
BASIN_STATIONS = [
    (-38.0, [(-38, 75.2), (-28, 66.0), (-22, 57.3), (-16, 49.9), (-10, 44.2), (-4, 40.3), (2, 38.6), (8, 39.4), (14, 41.7), (20, 45.7), (26, 51.1), (36, 56.5)]),
    (-22.0, [(-38, 77.4), (-28, 67.2), (-22, 58.9), (-16, 46.8), (-10, 39.0), (-4, 31.3), (2, 28.8), (8, 33.6), (14, 41.5), (20, 46.4), (26, 51.7), (36, 59.2)]),
    (-6.0, [(-38, 78.6), (-28, 63.9), (-22, 55.0), (-16, 44.6), (-10, 30.6), (-4, 21.0), (2, 19.5), (8, 24.2), (14, 35.4), (20, 44.6), (26, 50.9), (36, 61.6)]),
    (10.0, [(-38, 76.5), (-28, 59.9), (-22, 49.1), (-16, 40.6), (-10, 30.3), (-4, 22.2), (2, 22.8), (8, 27.8), (14, 38.0), (20, 45.5), (26, 52.0), (36, 62.9)]),
    (26.0, [(-38, 74.0), (-28, 60.3), (-22, 48.4), (-16, 41.1), (-10, 35.9), (-4, 32.6), (2, 34.7), (8, 39.7), (14, 44.8), (20, 48.3), (26, 54.0), (36, 61.2)]),
    (40.0, [(-38, 70.1), (-28, 59.6), (-22, 49.6), (-16, 43.2), (-10, 39.8), (-4, 40.2), (2, 41.8), (8, 44.3), (14, 46.7), (20, 49.8), (26, 54.5), (36, 59.1)]),
]
CUT_TOP = 120.0


def periodic_cubic(vals, theta_deg):
    """Periodic Catmull-Rom interpolation of equally spaced polar radii."""
    n = len(vals)
    t = (theta_deg % 360.0) / (360.0 / n)
    i = int(math.floor(t))
    f = t - i
    p0, p1, p2, p3 = (vals[(i + k) % n] for k in (-1, 0, 1, 2))
    return 0.5 * ((2 * p1) + (-p0 + p2) * f + (2 * p0 - 5 * p1 + 4 * p2 - p3) * f * f
                  + (-p0 + 3 * p1 - 3 * p2 + p3) * f ** 3)


def section_wire(z, cx, cy, radii):
    pts = []
    for k in range(N_PTS):
        th = SEAM_ANGLE + 360.0 * k / N_PTS
        r = periodic_cubic(radii, th)
        pts.append(cq.Vector(cx + r * math.cos(math.radians(th)),
                             cy + r * math.sin(math.radians(th)), z))
    return cq.Wire.assembleEdges([cq.Edge.makeSpline(pts, periodic=True)])


def smooth_loft(wire_list, max_degree=3, first_vertex=None):
    """Smooth (non-ruled) loft with a low-degree approximation to avoid wiggles."""
    b = BRepOffsetAPI_ThruSections(True, False, 1e-6)
    b.SetMaxDegree(max_degree)
    b.SetParType(Approx_ParametrizationType.Approx_Centripetal)
    if first_vertex is not None:
        b.AddVertex(BRepBuilderAPI_MakeVertex(gp_Pnt(*first_vertex)).Vertex())
    for w in wire_list:
        b.AddWire(w.wrapped)
    b.CheckCompatibility(False)
    b.Build()
    return cq.Solid(b.Shape())


# ---- body: smooth loft from the blunt tip up through all sections ----
wires = [section_wire(*s) for s in BODY_SECTIONS]
wires += [section_wire(z, CROWN_CENTER[0], CROWN_CENTER[1], CROWN_RADII) for z in CROWN_Z]
body = smooth_loft(wires, first_vertex=TIP)

# ---- basin cutter: loft of closed profiles normal to the basin axis ----
ca = math.cos(math.radians(BASIN_ANGLE))
sa = math.sin(math.radians(BASIN_ANGLE))
ox, oy = BASIN_ORIGIN


def to_xyz(u, v, z):
    return cq.Vector(ox + u * ca - v * sa, oy + u * sa + v * ca, z)


cut_wires = []
for (u, prof2d) in BASIN_STATIONS:
    prof = [to_xyz(u, v, z) for (v, z) in prof2d]
    v0, v1 = prof2d[0][0], prof2d[-1][0]
    sp = cq.Edge.makeSpline(prof)
    e1 = cq.Edge.makeLine(prof[-1], to_xyz(u, v1, CUT_TOP))
    e2 = cq.Edge.makeLine(to_xyz(u, v1, CUT_TOP), to_xyz(u, v0, CUT_TOP))
    e3 = cq.Edge.makeLine(to_xyz(u, v0, CUT_TOP), prof[0])
    cut_wires.append(cq.Wire.assembleEdges([sp, e1, e2, e3]))
# stations are lofted in reverse order so the basin face keeps an
# upward natural normal in the finished part
cutter = smooth_loft(cut_wires[::-1])

result = cq.Workplane("XY").add(body).cut(cq.Workplane("XY").add(cutter))
